import math
import cadquery as cq
from OCP.gp import gp_GTrsf, gp_Mat
from OCP.BRepBuilderAPI import BRepBuilderAPI_GTransform

# ---------------------------------------------------------------------------
# Space-shuttle stack kit laid out as separate printed bodies:
#   two open tank tubes, one cup (tube with floor), the tank nose ogive,
#   the orbiter (half fuselage with fin and engine bells) and two boosters.
# Every body is modelled round; the whole layout is then squeezed in Y by SY
# (the reference part is uniformly compressed across Y).
# Layout Y coordinates below are given AFTER the squeeze (as measured).
# ---------------------------------------------------------------------------
SY = 0.94                      # global Y compression of the layout

# tank tubes ---------------------------------------------------------------
TUBE_R = 38.3
TUBE_WALL = 4.6
TUBE_H = 77.3
CUP_H = 82.5
CUP_FLOOR = 4.0
TUBE_CHAMFER = 0.8             # bottom edge chamfer
TUBE_A_XY = (-80.8, 68.5)
TUBE_B_XY = (80.4, 65.3)
CUP_XY = (-80.4, -6.0)

# tank nose ogive ----------------------------------------------------------
NOSE_XY = (0.2, 63.8)
NOSE_R = 38.0
NOSE_MID = (27.0, 40.9)        # point on the ogive arc (r, z)
NOSE_TOP = (10.4, 73.3)        # truncation (r, z)
NOSE_TIP_R = 9.4
NOSE_TIP_Z = 81.5

# boosters (SRB) lying along X -----------------------------------------------
SRB_X0 = -112.9                # aft end
SRB_LEN = 218.9
SRB_ZC = 15.7                  # axis height
SRB_YS = (-57.6, -87.6)         # axis y at mid length (post squeeze)
SRB_YAW = 0.9                  # deg, boosters lie slightly skewed (nose +Y)
SRB_R = 13.2                   # forward body radius
SRB_RIB_R = 14.5               # segment ring radius
SRB_GROOVE = 1.0               # depth of the joint between rings
SRB_NECK_R = 13.3              # aft skirt body
SRB_LIP_R = 14.6               # aft skirt flange
SRB_LIP_L = 1.2
SRB_FLARE_L = 4.0
SRB_RIB_X0 = 25.0              # from aft end
SRB_RIB_N = 8
SRB_RIB_P = 9.2
SRB_NOSE_L = 28.7
SRB_TIP_R = 1.0

# orbiter ----------------------------------------------------------------------
ORB_X0 = -18.3
ORB_X1 = 102.0
ORB_Y0 = -6.25                 # centre line y at x = 0 (post squeeze)
ORB_YAW = 0.8                  # deg, orbiter lies slightly skewed (nose +Y)
ORB_A = 30.7 / SY              # half width (pre squeeze)
ORB_B = 23.0                   # height
ORB_Z0 = 6.2                   # flat underside height
ORB_CHAMFER = 1.0              # underside edge chamfer
ORB_GROOVES = (12.3, 35.2, 61.5)   # panel joints (absolute x)
ORB_SPLIT_X = 35.2             # joint that also crosses the underside
FIN_LE_T = 3.0                 # flat leading edge face width
FIN_TE_T = 1.4                 # trailing edge thickness
FIN_RIDGE = (0.22, 0.55)       # chord fractions of the facet ridges
FIN_RIDGE_T = (4.4, 5.0)       # thickness at the ridges (max thickness)
FIN_TOP_Z_TE = 83.5
FIN_TOP_Z_LE = 85.3
FIN_ROOT_Z = 24.0
FIN_TOP_TE = -31.6
FIN_TOP_LE = -23.6
FIN_TE_SWEEP = 0.248           # dx/dz (per unit drop in height)
FIN_LE_SWEEP = 0.68
OMS_R = 16.5                   # large aft pods (paraboloids)
OMS_X0 = -29.5
OMS_L = 32.0
OMS_DY = 18.3 / SY
OMS_Z = 24.0
KNOB_R = 4.4                   # OMS nozzle stub on the pod base
KNOB_L = 6.5
KNOB_DY = 8.6                  # outward offset from the pod axis
KNOB_DZ = 7.2                  # upward offset from the pod axis
SSME_R = 9.5                   # small engine bells under the tail
SSME_X0 = -36.0
SSME_L = 24.0
SSME_DY = 14.9 / SY
SSME_Z = 6.8


def scale_y(shape, sy):
    m = gp_Mat(1, 0, 0, 0, sy, 0, 0, 0, 1)
    g = gp_GTrsf()
    g.SetVectorialPart(m)
    b = BRepBuilderAPI_GTransform(shape, g, True)
    b.Build()
    return b.Shape()


def tube(xy, h, floor=0.0):
    cx, cy = xy[0], xy[1] / SY
    # seams turned to the silhouette of the usual views
    body = (cq.Workplane("XY").circle(TUBE_R).extrude(h)
            .faces("<Z").edges().chamfer(TUBE_CHAMFER))
    bore = (cq.Workplane("XY").workplane(offset=floor)
            .circle(TUBE_R - TUBE_WALL).extrude(h + 1))
    return (body.cut(bore).rotate((0, 0, 0), (0, 0, 1), 45)
            .translate((cx, cy, 0)))


def nose_cone():
    prof = (cq.Workplane("XZ")
            .moveTo(0, 0)
            .lineTo(NOSE_R, 0)
            .threePointArc(NOSE_MID, NOSE_TOP)
            .lineTo(NOSE_TIP_R, NOSE_TOP[1])
            .lineTo(0, NOSE_TIP_Z)
            .close())
    solid = prof.revolve(360, (0, 0, 0), (0, 1, 0))
    solid = solid.rotate((0, 0, 0), (0, 0, 1), 45)
    return solid.translate((NOSE_XY[0], NOSE_XY[1] / SY, 0))


def srb():
    """Booster: revolved (axial x, radius) profile about its own axis."""
    rr, g = SRB_RIB_R, SRB_GROOVE
    w = (cq.Workplane("XY").moveTo(0, 0).lineTo(0, SRB_LIP_R)
         .lineTo(SRB_LIP_L, SRB_LIP_R)
         .threePointArc((SRB_LIP_L + SRB_FLARE_L * 0.28, SRB_NECK_R + 0.55),
                        (SRB_LIP_L + SRB_FLARE_L, SRB_NECK_R))
         .lineTo(SRB_RIB_X0, SRB_NECK_R))
    # barrel-shaped segment rings
    for i in range(SRB_RIB_N):
        xa = SRB_RIB_X0 + i * SRB_RIB_P
        xb = xa + SRB_RIB_P
        if i == 0:
            w = w.lineTo(xa, rr - g)
        w = w.threePointArc(((xa + xb) / 2, rr), (xb, rr - g))
    xr = SRB_RIB_X0 + SRB_RIB_N * SRB_RIB_P
    xn = SRB_LEN - SRB_NOSE_L
    w = (w.lineTo(xr, SRB_R)
         .lineTo(xn, SRB_R)
         .lineTo(SRB_LEN - 0.5, SRB_TIP_R)
         .lineTo(SRB_LEN, 0)
         .close())
    s = w.revolve(360, (0, 0, 0), (1, 0, 0))
    s = s.rotate((0, 0, 0), (1, 0, 0), -45)
    return s.translate((SRB_X0, 0, SRB_ZC))


def bell(x0, length, r, y, z):
    """Engine bell / pod: flat base at x0 (aft), rounded nose pointing +X."""
    # paraboloid r = R*sqrt(1 - s), vertex at the nose
    pts = [(length * f, r * math.sqrt(1.0 - f)) for f in (0.3, 0.6, 0.85)]
    prof = (cq.Workplane("XY").moveTo(0, 0).lineTo(0, r)
            .spline(pts + [(length, 0)], tangents=[(1, -0.5), (0, -1)],
                    includeCurrent=True)
            .close())
    s = prof.revolve(360, (0, 0, 0), (1, 0, 0))
    return s.translate((x0, y, z))


def fin_section(x_te, x_le, z_te, z_le):
    """Faceted fin section (x along the chord, y thickness) on a slanted line."""
    c = x_le - x_te
    f0, f1 = FIN_RIDGE
    t0, t1 = FIN_RIDGE_T
    prof = [(0.0, FIN_TE_T / 2), (f0, t0 / 2), (f1, t1 / 2), (1.0, FIN_LE_T / 2)]
    pts = [(f, -t) for f, t in prof] + [(f, t) for f, t in reversed(prof)]
    return [cq.Vector(x_te + f * c, y, z_te + f * (z_le - z_te)) for f, y in pts]


def fin(ty):
    """Swept, tapered vertical fin with a faceted (bevelled) section."""
    zr = FIN_ROOT_Z
    te_r = FIN_TOP_TE + (FIN_TOP_Z_TE - zr) * FIN_TE_SWEEP
    le_r = FIN_TOP_LE + (FIN_TOP_Z_LE - zr) * FIN_LE_SWEEP
    root = cq.Wire.makePolygon(fin_section(te_r, le_r, zr, zr), close=True)
    tip = cq.Wire.makePolygon(fin_section(FIN_TOP_TE, FIN_TOP_LE,
                                          FIN_TOP_Z_TE, FIN_TOP_Z_LE), close=True)
    solid = cq.Solid.makeLoft([root, tip], True)
    return cq.Workplane("XY").newObject([solid]).translate((0, ty, 0))


def orbiter():
    """Orbiter built about its own centre line (y = 0)."""
    L = ORB_X1 - ORB_X0
    yc = 0.0
    ty = 0.0
    body = (cq.Workplane("YZ").workplane(offset=ORB_X0)
            .center(yc, ORB_Z0).ellipse(ORB_A, ORB_B).extrude(L))
    cutter = (cq.Workplane("XY").box(L + 10, 2 * ORB_A + 10, ORB_B + 5,
                                     centered=(False, True, False))
              .translate((ORB_X0 - 5, yc, ORB_Z0 - ORB_B - 5)))
    body = body.cut(cutter).faces("<Z").edges("|X").chamfer(ORB_CHAMFER)
    # shallow circumferential panel joints (the middle one runs right round)
    for gx in ORB_GROOVES:
        ring = (cq.Workplane("YZ").workplane(offset=gx - 0.3)
                .center(yc, ORB_Z0).ellipse(ORB_A + 2, ORB_B + 2)
                .ellipse(ORB_A - 0.5, ORB_B - 0.5).extrude(0.6))
        body = body.cut(ring)
    slot = (cq.Workplane("XY").box(0.6, 2 * ORB_A + 4, 0.5, centered=(True, True, False))
            .translate((ORB_SPLIT_X, yc, ORB_Z0)))
    body = body.cut(slot)
    # vertical fin: swept leading and trailing edges
    body = body.union(fin(ty))
    # OMS pods (large bells) on the upper aft corners, with nozzle stubs
    for s in (1, -1):
        py = ty + s * OMS_DY
        body = body.union(bell(OMS_X0, OMS_L, OMS_R, py, OMS_Z))
        knob = (cq.Workplane("YZ").workplane(offset=OMS_X0 - KNOB_L)
                .center(py + s * KNOB_DY, OMS_Z + KNOB_DZ)
                .circle(KNOB_R).extrude(KNOB_L + 0.5))
        body = body.union(knob)
    # main engines (small bells) under the aft end
    for s in (1, -1):
        body = body.union(bell(SSME_X0, SSME_L, SSME_R, ty + s * SSME_DY, SSME_Z))
    return body


def squeezed(wp):
    return [cq.Shape.cast(scale_y(s.wrapped, SY)) for s in wp.solids().vals()]


solids = []
for p in (tube(TUBE_A_XY, TUBE_H), tube(TUBE_B_XY, TUBE_H),
          tube(CUP_XY, CUP_H, CUP_FLOOR), nose_cone()):
    solids += squeezed(p)

for s in squeezed(orbiter()):
    solids.append(s.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), ORB_YAW)
                  .translate(cq.Vector(0, ORB_Y0, 0)))

srb_solid = squeezed(srb())[0]
srb_xc = SRB_X0 + SRB_LEN / 2
for y in SRB_YS:
    solids.append(srb_solid.rotate(cq.Vector(srb_xc, 0, 0), cq.Vector(srb_xc, 0, 1), SRB_YAW)
                  .translate(cq.Vector(0, y, 0)))

result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(solids)])

VIEW = {"azimuth": 45, "elevation": 26}
